import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R = 50.0                 # base / tower outer radius
HB = 27.5                # base height (z=0 at base bottom)
TOP = 167.0              # tower top height
X0 = 0.70 * R            # tower inner flat face (x)
XB = 0.78 * R            # back wall of the top cells (x)
W = math.sqrt(R * R - X0 * X0)   # tower half width
ZC = TOP - W             # centre of the dome sphere
RC = 0.66 * R            # radius of the cell window (cylinder along X)
RIB_T = 0.045 * R        # grid rib thickness
RIB_Y = 0.255 * R        # grid vertical rib position (+/-)
CELL_R = 0.05 * R        # cell corner radius
CORNER_R = 0.03 * R      # round on the tower's lower corner edges
CORNER_H = 1.72 * R      # height (above HB) of that round
CORNER_TAPER = 0.26 * R  # height over which the round fades out

BOSS_R = 0.62 * R        # raised disc on base top
BOSS_H = 0.08 * R

STRUT_YO = 0.48 * R      # strut outer face (+/-)
STRUT_YI0 = 0.39 * R     # strut inner face at the leg
STRUT_YI1 = 0.31 * R     # strut inner face at the tower
STRUT_XL = -0.78 * R     # strut outer (left) end
STRUT_Z0 = 0.33 * R      # strut top height (above HB) at left end corner
STRUT_SLOPE = 0.37
LEG_R = 0.14 * R         # round on the leg top corner
T1_X = 0.42 * R          # where the top line starts curving up
T2_H = 1.40 * R          # height above HB where the curve meets tower face
RIDGE_Y = 0.39 * R       # strut ridge line (+/-)
RIDGE_W = 0.045 * R      # width of the flat on the ridge
TAPER_X = -0.26 * R      # inner face reaches STRUT_YI1 here
PILLAR_T = 0.10 * R      # thickness of the fillet web rising up the tower
WIN_X1, WIN_X2 = -0.53 * R, 0.51 * R
WIN_H = 0.265 * R        # window top above HB
WIN_R = 0.09 * R

POCKET_X1, POCKET_X2 = -0.66 * R, 0.60 * R
POCKET_Y = 0.30 * R
POCKET_D = 0.12 * R
BLOCK_X = 0.58 * R       # central block front face
BLOCK_DROP = 0.15 * R    # central block top below strut top

CHEEK_T = 0.05 * R       # cheek wall thickness
CHEEK_H_NEG = 0.29 * R   # cheek height at tower corner, -Y side
CHEEK_H_POS = 0.60 * R   # cheek height at tower corner, +Y side

SEAM_Z = HB - 0.06 * R   # small groove below the base top
NOTCH_W = 0.14 * R
NOTCH_H = 0.08 * R
NOTCH_D = 0.03 * R

BOLT_R = 0.88 * R
BOLT_D = 0.072 * R

BOT_RING_R = 0.74 * R
BOT_RING_H = 4.9
BOT_DISC_R = 0.60 * R
BOT_DISC_H = 3.8

TAB_W = 0.30 * R
FL_A1, FL_A2 = -140.0, -40.0   # angular span of the bottom flange
FLANGE_H = 0.07 * R
RIB_B_H = 0.025 * R
TAB_H = 0.29 * R

HOLE_X = 0.878 * R
HOLE_D = 0.075 * R
CBORE_D = 0.16 * R


def box(x1, x2, y1, y2, z1, z2):
    return (cq.Workplane("XY")
            .box(x2 - x1, y2 - y1, z2 - z1, centered=False)
            .translate((x1, y1, z1)))


def disc(r, z1, z2, rot=180.0):
    # cylinder with its seam turned away from the main views
    return (cq.Workplane("XY").workplane(offset=z1)
            .transformed(rotate=(0, 0, rot)).circle(r).extrude(z2 - z1))


# ---------------- base ----------------
base = disc(R, 0, HB)
base = base.union(disc(BOSS_R, HB - 0.5, HB + BOSS_H))
base = base.union(disc(BOT_RING_R, -BOT_RING_H, 0.5))
base = base.union(disc(BOT_DISC_R, -BOT_RING_H - BOT_DISC_H, -BOT_RING_H + 0.5))

# thin arc-shaped flange under the base on the -Y side
a1, a2 = math.radians(FL_A1), math.radians(FL_A2)
am = 0.5 * (a1 + a2)
flange = (cq.Workplane("XY").workplane(offset=-FLANGE_H)
          .moveTo(BOT_RING_R * math.cos(a1), BOT_RING_R * math.sin(a1))
          .lineTo(R * math.cos(a1), R * math.sin(a1))
          .threePointArc((R * math.cos(am), R * math.sin(am)), (R * math.cos(a2), R * math.sin(a2)))
          .lineTo(BOT_RING_R * math.cos(a2), BOT_RING_R * math.sin(a2))
          .threePointArc((BOT_RING_R * math.cos(am), BOT_RING_R * math.sin(am)),
                         (BOT_RING_R * math.cos(a1), BOT_RING_R * math.sin(a1)))
          .close().extrude(FLANGE_H + 0.5))
base = base.union(flange)

# small radial ribs on the underside running out to the bottom bolt holes
for ang in (0.0, 45.0, 90.0, 135.0, 180.0):
    rib = (box(BOT_RING_R - 1.0, 0.96 * R, -0.035 * R, 0.035 * R, -RIB_B_H, 0.5)
           .rotate((0, 0, 0), (0, 0, 1), ang))
    base = base.union(rib)

# tab hanging below the flange on the -Y side (trapezoid in side and front view)
tab_side = (cq.Workplane("YZ", origin=(-R, 0, 0))
            .polyline([(-0.70 * R, -FLANGE_H + 0.5), (-1.0 * R, -FLANGE_H + 0.5),
                       (-1.0 * R, -FLANGE_H - 0.03 * R), (-0.93 * R, -TAB_H),
                       (-0.74 * R, -TAB_H), (-0.70 * R, -FLANGE_H - 0.05 * R)]).close()
            .extrude(2 * R))
tab_front = (cq.Workplane("XZ", origin=(0, 0, 0))
             .polyline([(-TAB_W / 2, -FLANGE_H + 0.5), (TAB_W / 2, -FLANGE_H + 0.5),
                        (0.09 * R, -TAB_H), (-0.09 * R, -TAB_H)]).close()
             .extrude(R + 1, both=True))
tab = tab_side.intersect(tab_front)
base = base.union(tab)

# shallow groove just below the top rim
groove = disc(R + 1, SEAM_Z - 0.35, SEAM_Z + 0.35).cut(disc(R - 0.5, SEAM_Z - 1, SEAM_Z + 1))
base = base.cut(groove)

# snap notches around the rim
for k in range(8):
    a = 22.5 + 45.0 * k
    n = (box(R - NOTCH_D, R + 1, -NOTCH_W / 2, NOTCH_W / 2, SEAM_Z - NOTCH_H, SEAM_Z)
         .rotate((0, 0, 0), (0, 0, 1), a))
    base = base.cut(n)

# shallow rounded pocket in the boss between the struts
pocket = (cq.Workplane("XY").workplane(offset=HB + BOSS_H - POCKET_D)
          .center((POCKET_X1 + POCKET_X2) / 2, 0)
          .rect(POCKET_X2 - POCKET_X1, 2 * POCKET_Y).extrude(POCKET_D + 1))
pocket = pocket.edges("|Z").fillet(0.12 * R)
base = base.cut(pocket)

# ---------------- tower ----------------
cyl = disc(R, 0, ZC, rot=0.0)
dome = cq.Workplane("XY").sphere(R).translate((0, 0, ZC))
tower = cyl.union(dome).intersect(box(X0, R + 1, -R - 1, R + 1, HB - 1, TOP + 1))

# round the two vertical corner edges of the tower in its lower part
def corner_round_tool(r, z1, z2):
    cy = -math.sqrt((R - r) ** 2 - (X0 + r) ** 2)       # fillet centre (-Y corner)
    c = (X0 + r, cy)
    k = R / (R - r)
    tc = (c[0] * k, c[1] * k)                            # tangent point on the circle
    far = (X0 - 1.0, -R - 1.0)
    pts = [c, (X0 - 1.0, cy), far, (tc[0] + 0.3 * (tc[0] - c[0]) / r * 5, tc[1] + 0.3 * (tc[1] - c[1]) / r * 5)]
    wedge = (cq.Workplane("XY").workplane(offset=z1).polyline(pts).close().extrude(z2 - z1))
    circ = cq.Workplane("XY").workplane(offset=z1 - 1).center(*c).circle(r).extrude(z2 - z1 + 2)
    return wedge.cut(circ)


def corner_tool_tapered():
    t = corner_round_tool(CORNER_R, HB - 1, HB + CORNER_H)
    # tapered run-out above CORNER_H: the round fades out toward the corner tip
    cy = -math.sqrt((R - CORNER_R) ** 2 - (X0 + CORNER_R) ** 2)
    c = (X0 + CORNER_R, cy)
    p = (X0, -W)
    d = math.hypot(p[0] - c[0], p[1] - c[1])
    u = ((p[0] - c[0]) / d, (p[1] - c[1]) / d)
    k = CORNER_TAPER / (d - CORNER_R)
    top = corner_round_tool(CORNER_R, HB + CORNER_H - 0.01, HB + CORNER_H + CORNER_TAPER)
    n = cq.Vector(-k * u[0], -k * u[1], 1.0).normalized()
    org = cq.Vector(c[0] + u[0] * CORNER_R, c[1] + u[1] * CORNER_R, HB + CORNER_H)
    pl = cq.Plane(origin=org, xDir=cq.Vector(-u[1], u[0], 0), normal=n)
    below = cq.Workplane(pl).rect(60, 60).extrude(-40)
    return t.union(top.intersect(below))


ctool = corner_tool_tapered()
tower = tower.cut(ctool).cut(ctool.mirror("XZ"))
# half width of the tower below the corner round
W_LOW = abs(-math.sqrt((R - CORNER_R) ** 2 - (X0 + CORNER_R) ** 2) * R / (R - CORNER_R))

# cell window: cylinder along X, minus ribs (6 cells)
cell = (cq.Workplane("YZ").workplane(offset=XB)
        .center(0, ZC).circle(RC).extrude(R))
ribs = (box(XB - 1, R + 2, -RIB_Y - RIB_T / 2, -RIB_Y + RIB_T / 2, ZC - RC - 2, ZC + RC + 2)
        .union(box(XB - 1, R + 2, RIB_Y - RIB_T / 2, RIB_Y + RIB_T / 2, ZC - RC - 2, ZC + RC + 2))
        .union(box(XB - 1, R + 2, -RC - 2, RC + 2, ZC - RIB_T / 2, ZC + RIB_T / 2)))
cell = cell.cut(ribs)
try:
    cell = cell.edges("|X").fillet(CELL_R)
except Exception:
    pass
tower = tower.cut(cell)


# ---------------- gussets (struts + central block) ----------------
def gusset_profile(xl, zl, rl, x_t1, z_t2):
    """XZ outline: vertical front at xl, sloped top (STRUT_SLOPE) with convex
    round rl at the front, then a tangent curve rising into the tower face."""
    al = math.atan(STRUT_SLOPE)
    ca, sa = math.cos(al), math.sin(al)
    t1 = (x_t1, zl + STRUT_SLOPE * (x_t1 - xl))
    t2 = (X0, z_t2)
    wp = cq.Workplane("XZ").moveTo(xl, HB - 0.5)
    if rl > 0:
        phi = math.pi / 2 - al
        dl = rl * math.tan(phi / 2)
        s1 = (xl, zl - dl)
        s2 = (xl + dl * ca, zl + dl * sa)
        cl = (xl + rl, zl - dl)
        vl = (-rl, dl)
        nl = math.hypot(*vl)
        ml = (cl[0] + rl * vl[0] / nl, cl[1] + rl * vl[1] / nl)
        wp = wp.lineTo(*s1).threePointArc(ml, s2)
    else:
        wp = wp.lineTo(xl, zl)
    wp = (wp.lineTo(*t1)
          .spline([t2], tangents=[(ca, sa), (0, 1)], includeCurrent=True)
          .lineTo(X0 + 0.5, t2[1]).lineTo(X0 + 0.5, HB - 0.5).close())
    return wp


def slab(prof, y1, y2):
    # XZ workplane normal is -Y: extrude then shift so it spans y1..y2
    return prof.extrude(y2 - y1).translate((0, y2, 0))


z_l = HB + STRUT_Z0



def strut(sign):
    s = slab(gusset_profile(STRUT_XL, z_l, LEG_R, T1_X, HB + T2_H), STRUT_YI1, STRUT_YO)
    # plan taper of the inner face near the leg
    taper = (cq.Workplane("XY").workplane(offset=-1)
             .polyline([(STRUT_XL - 1, STRUT_YI0 + 0.01 * R), (TAPER_X, STRUT_YI1),
                        (X0 + 2, STRUT_YI1), (X0 + 2, STRUT_YO + 1),
                        (STRUT_XL - 1, STRUT_YO + 1)]).close()
             .extrude(TOP))
    s = s.intersect(taper)
    # ridged "roof": sloped faces from the ridge down to the window-top level
    zA = HB + WIN_H
    x1, x2 = STRUT_XL - 1.0, X0 + 1.0

    def sec(x):
        zr = z_l + STRUT_SLOPE * (x - STRUT_XL)
        return [(STRUT_YI1 - 2, HB - 2), (STRUT_YI1 - 2, zA - 0.02 * R),
                (STRUT_YI1, zA), (RIDGE_Y - RIDGE_W / 2, zr), (RIDGE_Y + RIDGE_W / 2, zr),
                (STRUT_YO, zA), (STRUT_YO + 2, zA - 0.02 * R), (STRUT_YO + 2, HB - 2)]
    roof = (cq.Workplane("YZ").workplane(offset=x1).polyline(sec(x1)).close()
            .workplane(offset=x2 - x1).polyline(sec(x2)).close().loft(ruled=True))
    keep = roof.union(box(T1_X - 0.05 * R, X0 + 2, RIDGE_Y - PILLAR_T / 2,
                          RIDGE_Y + PILLAR_T / 2, HB - 2, TOP))
    s = s.intersect(keep)
    if sign < 0:
        s = s.mirror("XZ")
    return s


struts = strut(1).union(strut(-1))

# windows under the struts
win = (cq.Workplane("XZ", origin=(0, R, 0))
       .center((WIN_X1 + WIN_X2) / 2, HB + WIN_H / 2 - 0.25)
       .rect(WIN_X2 - WIN_X1, WIN_H + 0.5).extrude(2 * R))
win = win.edges("|Y").fillet(WIN_R)
struts = struts.cut(win)

# central block between struts, against the tower face
zb = z_l - BLOCK_DROP + STRUT_SLOPE * (BLOCK_X - STRUT_XL)
block = slab(gusset_profile(BLOCK_X, zb, 0.0, T1_X, HB + T2_H - BLOCK_DROP),
             -STRUT_YI1 - 0.5, STRUT_YI1 + 0.5)

gus = struts.union(block)


# ---------------- cheek walls at the tower corners ----------------
def cheek_solid(h, sign):
    y0 = W_LOW - 1.6
    ry = R - W_LOW
    # 2D region in YZ: rectangle minus a quarter ellipse, extruded along X
    rect = (cq.Workplane("YZ").workplane(offset=-1)
            .center((y0 + R + 2) / 2, HB - 0.5 + (h + 0.5) / 2)
            .rect(R + 2 - y0, h + 0.5).extrude(X0 + 6))
    ell = (cq.Workplane("YZ").workplane(offset=-2)
           .center(R, HB + h).ellipse(ry, h).extrude(X0 + 8))
    c = rect.cut(ell)
    ring = (disc(R, HB - 0.5, HB + h + 1, rot=0.0)
            .cut(disc(R - CHEEK_T, HB - 1, HB + h + 2, rot=0.0)))
    keep = ring.union(box(X0, X0 + 4.0, y0, R + 1, HB - 1, HB + h + 1))
    c = c.intersect(keep).intersect(disc(R, HB - 1, HB + h + 1, rot=0.0))
    c = c.intersect(box(0, X0 + 4.0, y0, R + 1, HB - 1, HB + h + 1))
    if sign < 0:
        c = c.mirror("XZ")
    return c


cheeks = cheek_solid(CHEEK_H_POS, 1).union(cheek_solid(CHEEK_H_NEG, -1))

body = base.union(tower.union(cheeks)).union(gus)

# ---------------- holes ----------------
for ang in (45, 90, 135, 225, 270, 315):
    a = math.radians(ang)
    h = (cq.Workplane("XY").workplane(offset=HB - 12)
         .center(BOLT_R * math.cos(a), BOLT_R * math.sin(a)).circle(BOLT_D / 2).extrude(14))
    body = body.cut(h)

# blind holes on the underside, 8x on the same bolt circle
for k in range(8):
    a = math.radians(45.0 * k)
    h = (cq.Workplane("XY").workplane(offset=-1)
         .center(BOLT_R * math.cos(a), BOLT_R * math.sin(a)).circle(BOLT_D / 2).extrude(7))
    body = body.cut(h)

# vertical holes in the tower cells (coaxial)
for zf in (ZC + RIB_T / 2, ZC - RC):
    cb = (cq.Workplane("XY").workplane(offset=zf - 1.2)
          .center(HOLE_X, 0).circle(CBORE_D / 2).extrude(3))
    hl = (cq.Workplane("XY").workplane(offset=zf - 12)
          .center(HOLE_X, 0).circle(HOLE_D / 2).extrude(13))
    body = body.cut(cb).cut(hl)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
